import math
import cadquery as cq

# Spur gear (25 teeth, module 2) with a plain hub on the -X side, a concave
# blend from the hub into the gear face, and a deep blind bore from the hub end.
# Gear axis = X, hub toward -X, one tooth pointing +Y.

# ---------------- driving dimensions (mm) ----------------
MODULE = 2.0            # gear module
TEETH = 25              # number of teeth
FACE_WIDTH = 40.0       # toothed length along +X
TIP_LAND = 1.6          # chordal width of the flat tooth tip
ROOT_WIDTH = 3.95       # chordal tooth width where the flank meets the root circle
FLANK_BULGE = 0.15      # convexity of each flank at mid height

HUB_DIA = 43.5          # plain hub on the -X side (just under the root circle)
HUB_LEN = 8.0
HUB_FILLET = 2.0        # hub -> gear-face blend radius (tooth spaces run through it)

BORE_DIA = 37.0         # blind bore entering from the hub end
BORE_DEPTH = 40.0       # measured from the hub end face

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
R_TIP = MODULE * (TEETH + 2) / 2.0          # 27.0  addendum circle
R_ROOT = MODULE * (TEETH - 2.5) / 2.0       # 22.5  dedendum circle
PITCH_ANG = 2 * math.pi / TEETH

X = cq.Vector(1, 0, 0)
O = cq.Vector(0, 0, 0)


def yz(r, th):
    """point in the YZ plane (gear axis = X); th measured from +Y toward +Z"""
    return cq.Vector(0.0, r * math.cos(th), r * math.sin(th))


def gear_profile():
    """closed tooth outline: root arcs, slightly convex flanks, flat tips"""
    psi_a = math.asin((TIP_LAND / 2) / R_TIP)          # half tip angle
    psi_f = math.asin((ROOT_WIDTH / 2) / R_ROOT)       # half root angle
    r_m = 0.5 * (R_TIP + R_ROOT)
    w_m = 0.5 * (TIP_LAND / 2 + ROOT_WIDTH / 2) + FLANK_BULGE
    psi_m = math.asin(w_m / r_m)
    edges = []
    for k in range(TEETH):
        th = k * PITCH_ANG
        a0, a1 = yz(R_ROOT, th - psi_f), yz(R_TIP, th - psi_a)
        b0, b1 = yz(R_TIP, th + psi_a), yz(R_ROOT, th + psi_f)
        edges.append(cq.Edge.makeThreePointArc(a0, yz(r_m, th - psi_m), a1))  # flank
        edges.append(cq.Edge.makeThreePointArc(a1, yz(R_TIP, th), b0))        # tip
        edges.append(cq.Edge.makeThreePointArc(b0, yz(r_m, th + psi_m), b1))  # flank
        nxt = yz(R_ROOT, th + PITCH_ANG - psi_f)
        edges.append(cq.Edge.makeThreePointArc(b1, yz(R_ROOT, th + PITCH_ANG / 2), nxt))
    return cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))


# ---------------- toothed body ----------------
profile = gear_profile()
gear = cq.Solid.extrudeLinear(profile, cq.Vector(FACE_WIDTH, 0, 0))

# ---------------- hub + blend (one revolved surface) ----------------
# profile in the XY half-plane (r along +Y): straight hub line, then a
# quarter-round blend tangent to the hub and to the gear face
rh = HUB_DIA / 2
F = HUB_FILLET
cx, cy = -F, rh + F                           # blend centre
pts = [cq.Vector(-HUB_LEN, rh, 0)]
tans = [cq.Vector(1, 0, 0)]
for k in range(5):
    ph = math.radians(22.5 * k)
    pts.append(cq.Vector(cx + F * math.sin(ph), cy - F * math.cos(ph), 0))
    tans.append(cq.Vector(math.cos(ph), math.sin(ph), 0))
e_side = cq.Edge.makeSpline(pts, tangents=tans)
e_end = cq.Edge.makeLine(cq.Vector(-HUB_LEN, 0, 0), cq.Vector(-HUB_LEN, rh, 0))
e_top = cq.Edge.makeLine(cq.Vector(0, rh + F, 0), cq.Vector(0.5, rh + F, 0))
e_cap = cq.Edge.makeLine(cq.Vector(0.5, rh + F, 0), cq.Vector(0.5, 0, 0))
e_axis = cq.Edge.makeLine(cq.Vector(0.5, 0, 0), cq.Vector(-HUB_LEN, 0, 0))
hub_sec = cq.Face.makeFromWires(cq.Wire.assembleEdges([e_end, e_side, e_top, e_cap, e_axis]))
hub = cq.Solid.revolve(hub_sec, 360, O, X).rotate(O, X, -90)   # seam parked at -Z

# the tooth spaces run straight through the blend: keep it only under the teeth
clip = cq.Solid.extrudeLinear(profile, cq.Vector(-(HUB_LEN + 1.0), 0, 0)).translate(
    cq.Vector(0.5, 0, 0))
hub = hub.intersect(clip)

body = gear.fuse(hub).clean()

# ---------------- blind bore from the hub end ----------------
bore = cq.Solid.makeCylinder(BORE_DIA / 2, BORE_DEPTH, cq.Vector(-HUB_LEN, 0, 0), X)
body = body.cut(bore).clean()

result = cq.Workplane("XY").add(body.Solids())
